import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 40.0          # width of the clevis plates
H = 44.7          # overall height (Z)
T = 6.4           # prong plate thickness
LC = 100.4        # eye (hole) centre to rear end face
R_END = W / 2.0   # rounded eye end radius
D_HOLE = 21.3     # eye hole diameter
R_HOLE = 0.4      # small rounding of the eye hole rims

U1 = 45.5         # gusset wall meets the closed (+Y local) side, measured from eye centre
U2 = 91.5         # gusset wall meets the open (-Y local) side, measured from eye centre
R_V = 2.5         # rounding of the two vertical gusset edges
R_D = 2.0         # fillet between gusset wall and prongs

PIN_D = 4.8       # dowel pins on the rear face
PIN_L = 6.2
PIN_IN = 8.0      # pin inset from the face edges

ROT = 21.9        # the part is turned about Z by this angle (deg)

# ---------------- body: plate with a round eye end ----------------
body = (
    cq.Workplane("XY")
    .moveTo(0, -W / 2)
    .lineTo(LC, -W / 2)
    .lineTo(LC, W / 2)
    .lineTo(0, W / 2)
    .threePointArc((-R_END, 0), (0, -W / 2))
    .close()
    .extrude(H)
)

# eye holes through both prongs
body = body.cut(cq.Workplane("XY").circle(D_HOLE / 2).extrude(H))

# ---------------- slot between the prongs ----------------
# The slot ends in a diagonal gusset wall running from (U1, +W/2) to (U2, -W/2).
# Its two vertical ends are rounded (R_V) and its joints with the prongs filleted (R_D).
dx, dy = U2 - U1, -W
dl = math.hypot(dx, dy)
ux, uy = dx / dl, dy / dl
alpha = math.atan2(-uy, ux)          # acute wedge at the closed side
beta = math.pi - alpha               # obtuse wedge at the open side
t1 = R_V / math.tan(alpha / 2)
t2 = R_V / math.tan(beta / 2)
P1 = (U1 + t1, W / 2)
Q1 = (U1 + t1 * ux, W / 2 + t1 * uy)
C1 = (U1 + t1, W / 2 - R_V)
P4 = (U2 + t2, -W / 2)
Q4 = (U2 - t2 * ux, -W / 2 - t2 * uy)
C4 = (U2 + t2, -W / 2 + R_V)


def _arc_mid(c, a, b, r):
    a1 = math.atan2(a[1] - c[1], a[0] - c[0])
    a2 = math.atan2(b[1] - c[1], b[0] - c[0])
    while a2 < a1:
        a2 += 2 * math.pi
    am = 0.5 * (a1 + a2)
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


M1 = _arc_mid(C1, P1, Q1, R_V)
M4 = _arc_mid(C4, Q4, P4, R_V)

E = 10.0
slot = (
    cq.Workplane("XY")
    .workplane(offset=T)
    .moveTo(-R_END - E, W / 2 + E)
    .lineTo(P1[0], W / 2 + E)
    .lineTo(*P1)
    .threePointArc(M1, Q1)
    .lineTo(*Q4)
    .threePointArc(M4, P4)
    .lineTo(P4[0], -W / 2 - E)
    .lineTo(-R_END - E, -W / 2 - E)
    .close()
    .extrude(H - 2 * T)
)
slot_edges = slot.faces(">Z").edges().vals() + slot.faces("<Z").edges().vals()
slot_solid = slot.val().fillet(R_D, slot_edges)
body = body.cut(cq.Workplane("XY").add(slot_solid))

# soften the four eye-hole rims
if R_HOLE > 0:
    rims = [
        e
        for e in body.edges("%CIRCLE").vals()
        if abs(e.radius() - D_HOLE / 2) < 1e-6
    ]
    body = cq.Workplane("XY").add(body.val().fillet(R_HOLE, rims))

# ---------------- dowel pins on the rear face ----------------
pins = (
    cq.Workplane("YZ", origin=(LC, 0, 0))
    .pushPoints(
        [
            (y, z)
            for y in (-W / 2 + PIN_IN, W / 2 - PIN_IN)
            for z in (PIN_IN, H - PIN_IN)
        ]
    )
    .circle(PIN_D / 2)
    .extrude(PIN_L)
)
body = body.union(pins)

# ---------------- orientation as in the reference ----------------
body = body.translate((-(LC - R_END) / 2, 0, -H / 2)).rotate((0, 0, 0), (0, 0, 1), ROT)

result = body
